import cadquery as cq

# ---------------------------------------------------------------
# Four-pad vacuum lifter.  The four suction pads lie in the XZ plane
# (glass-side face at +Y), the hand pump / gauge / battery box and
# the four lever handles sit on the -Y side, a small space frame runs
# through the gap between the pads to a box behind them.
# All sizes are written in design units "u" and scaled with K -> mm.
# ---------------------------------------------------------------
K = 2.0                      # mm per design unit


def u(v):
    return v * K


PAD_PITCH = u(61.6)          # pad centre offset from middle (X and Z)
PAD_R = u(57.0)              # pad radius
PAD_T = u(12.0)              # pad thickness (Y 0 .. +PAD_T)

HUB_R = u(11.5)              # hub on the pad front
HUB_L = u(16.0)
COLLAR_R = u(12.2)           # thin ring carrying the frame arms
COLLAR_L = u(4.0)

HANDLE_Y0 = u(-17.0)         # lever root
HANDLE_Y1 = u(-85.5)         # lever tip
HCH = 0.7                    # corner cut of the lever section (0=box, 1=diamond)

ARM_Y0, ARM_Y1 = u(-20.0), u(-14.0)

PUMP_Y = u(-53.7)            # twin pump barrels (axis along X)
PUMP_Z = u(9.4)
PUMP_R = u(9.4)

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- primitive helpers ---------------------------
def box(x0, x1, y0, y1, z0, z1):
    x0, x1 = min(x0, x1), max(x0, x1)
    y0, y1 = min(y0, y1), max(y0, y1)
    z0, z1 = min(z0, z1), max(z0, z1)
    return cq.Workplane("XY").add(
        cq.Solid.makeBox(x1 - x0, y1 - y0, z1 - z0, cq.Vector(x0, y0, z0)))


def cyl_x(y, z, r, x0, x1):
    return cq.Workplane("XY").add(
        cq.Solid.makeCylinder(r, x1 - x0, cq.Vector(x0, y, z), cq.Vector(1, 0, 0)))


def cyl_y(x, z, r, y0, y1):
    return cq.Workplane("XY").add(
        cq.Solid.makeCylinder(r, y1 - y0, cq.Vector(x, y0, z), cq.Vector(0, 1, 0)))


def cyl_z(x, y, r, z0, z1):
    return cq.Workplane("XY").add(
        cq.Solid.makeCylinder(r, z1 - z0, cq.Vector(x, y, z0), cq.Vector(0, 0, 1)))


def rod(p0, p1, r):
    a, b = cq.Vector(*p0), cq.Vector(*p1)
    d = b - a
    return cq.Workplane("XY").add(cq.Solid.makeCylinder(r, d.Length, a, d.normalized()))


# ---------------- pads, hubs and handles -----------------------
def pad(xc, zc):
    p = cq.Workplane("XZ", origin=(xc, 0, zc)).circle(PAD_R).extrude(-PAD_T)
    p = p.faces(">Y").edges().chamfer(u(0.8))
    p = p.faces("<Y").edges().chamfer(u(0.5))
    hub = cyl_y(xc, zc, HUB_R, -HUB_L, 0.0)
    col = cyl_y(xc, zc, COLLAR_R, -HUB_L - COLLAR_L, -HUB_L)
    ring = cyl_y(xc, zc, COLLAR_R + u(0.6), -HUB_L - COLLAR_L - u(1.0),
                 -HUB_L - COLLAR_L + u(1.5))
    return p.union(hub).union(col).union(ring)


def octagon(yc, cx, cz, a, b, c):
    """Closed wire in the plane Y=yc: rectangle 2a x 2b (X x Z) centred on
    (cx, cz) with corners cut by c (a chamfered, faceted lever section)."""
    pts = [(a, b - c), (a - c, b), (-a + c, b), (-a, b - c),
           (-a, -b + c), (-a + c, -b), (a - c, -b), (a, -b + c)]
    return cq.Wire.makePolygon(
        [cq.Vector(cx + x, yc, cz + z) for x, z in pts], close=True)


def handle_top_right():
    """Lever for the pad at (+X,+Z); local coords relative to hub centre.
    The lever tapers towards the middle of the lifter (-X and -Z)."""
    # (Y, centre X, centre Z, half X, half Z) stations along the lever
    st = [(HANDLE_Y0, -0.85, -0.4, 9.85, 9.9),
          (u(-40.0), -1.65, -1.15, 8.85, 9.15),
          (u(-63.0), -3.5, -3.0, 6.7, 7.3),
          (HANDLE_Y1, -6.95, -5.75, 2.95, 4.55)]
    secs = [octagon(y, u(cx), u(cz), u(a), u(b), u(min(a, b) * HCH))
            for y, cx, cz, a, b in st]
    return cq.Workplane("XY").add(cq.Solid.makeLoft(secs, False))


parts = []
lever_tr = handle_top_right()
for sx in (1, -1):
    for sz in (1, -1):
        xc, zc = sx * PAD_PITCH, sz * PAD_PITCH
        parts.append(pad(xc, zc))
        lv = lever_tr
        if sx < 0:
            lv = lv.mirror("YZ")
        if sz < 0:
            lv = lv.mirror("XY")
        parts.append(lv.translate((xc, 0, zc)))


# ---------------- frame arms (flat bands on the hub collars) ---
def band(pts, y0=ARM_Y0, y1=ARM_Y1):
    return (cq.Workplane("XZ", origin=(0, y1, 0)).polyline(pts).close()
            .extrude(y1 - y0))


for sx in (1, -1):
    # lower arms: hub collar -> side of the block
    pts = [(sx * u(57), u(-49.4)), (sx * u(31), u(-24.5)),
           (sx * u(31), u(-39.4)), (sx * u(49.7), u(-56.1)),
           (sx * u(61.6), u(-61.6))]
    parts.append(band(pts))
    # upper arms: hub collar -> end of the crossbar
    pts = [(sx * u(55), u(55)), (sx * u(46), u(50.5)),
           (sx * u(46), u(40)), (sx * u(61.6), u(50))]
    parts.append(band(pts, u(-26), ARM_Y1))

# ---------------- space frame through the pad gap -------------
FR = 1.3  # rod radius (u)


def frame_box(x0, x1, y0, y1, z0, z1, braces):
    xs, ys, zs = (u(x0), u(x1)), (u(y0), u(y1)), (u(z0), u(z1))
    out = []
    for y in ys:
        for z in zs:
            out.append(rod((xs[0], y, z), (xs[1], y, z), u(FR)))
    for x in xs:
        for z in zs:
            out.append(rod((x, ys[0], z), (x, ys[1], z), u(FR)))
        for y in ys:
            out.append(rod((x, y, zs[0]), (x, y, zs[1]), u(FR)))
    for a, b in braces:
        out.append(rod(a, b, u(FR * 0.8)))
    return out


# upper core frame (crosses the pad plane), X-braced on top
cx0, cx1, cy0, cy1, cz0, cz1 = -15.8, 18.8, -13.0, 21.7, -12.5, 27.5
br = [((u(cx0), u(cy0), u(cz1)), (u(cx1), u(cy1), u(cz1))),
      ((u(cx1), u(cy0), u(cz1)), (u(cx0), u(cy1), u(cz1)))]
for x in (u(cx0), u(cx1)):
    br.append(((x, u(cy0), u(cz0)), (x, u(4.0), u(cz1))))
    br.append(((x, u(cy1), u(cz0)), (x, u(4.0), u(cz1))))
br.append(((u(cx0), u(cy1), u(cz0)), (u(cx1), u(cy1), u(cz1))))
parts += frame_box(cx0, cx1, cy0, cy1, cz0, cz1, br)

# lower, wider frame around the core
rx0, rx1, rz1 = -28.0, 29.0, 6.0
br = []
for x0_, x1_ in ((rx0, cx0), (rx1, cx1)):
    br.append(((u(x0_), u(cy1), u(cz0)), (u(x1_), u(cy1), u(rz1))))
    br.append(((u(x0_), u(cy0), u(cz0)), (u(x1_), u(cy0), u(rz1))))
    br.append(((u(x0_), u(cy0), u(rz1)), (u(x0_), u(cy1), u(cz0))))
parts += frame_box(rx0, rx1, cy0, cy1, cz0, rz1, br)

# box hanging behind the pads
parts.append(box(u(-8), u(8), u(12.7), u(24.2), u(-41), u(-21.5)))
parts.append(box(u(-3), u(3), u(19), u(23), u(-22), u(-13)))
# small block on top of the rear frame
parts.append(box(u(-9.6), u(7.7), u(17), u(25), u(26), u(30)))

# front plate of the core (mechanism mounting plate)
parts.append(box(u(cx0), u(cx1), u(-14.5), u(-12.5), u(cz0), u(cz1)))

# ---------------- crossbar with two vertical caps -------------
CB = dict(x0=u(-50), x1=u(61), y0=u(-49), y1=u(-23), z0=u(35.5), z1=u(49.3))
crossbar = box(CB["x0"], CB["x1"], CB["y0"], CB["y1"], CB["z0"], CB["z1"])
crossbar = crossbar.edges("|Z").fillet(u(5))
for xe, d in ((CB["x1"], -u(2)), (CB["x0"], u(2))):
    slot = (cq.Workplane("YZ", origin=(xe, 0, 0))
            .center((CB["y0"] + CB["y1"]) / 2, (CB["z0"] + CB["z1"]) / 2)
            .slot2D(u(10), u(4)).extrude(d))
    crossbar = crossbar.cut(slot)
# raised lip along the front edge of the crossbar
lip = box(CB["x0"] + u(5), CB["x1"] - u(5), CB["y0"], CB["y0"] + u(1.5),
          CB["z1"], CB["z1"] + u(1.5))
parts.append(crossbar.union(lip))
for sx in (1, -1):
    parts.append(cyl_z(sx * u(27.5), u(-37), u(8.4), CB["z1"], u(64.4)))

# rounded housing under the crossbar
hump = box(u(-29), u(30), u(-53), u(-24), u(30), u(50))
hump = hump.edges("|Y").edges(">Z").fillet(u(8))
parts.append(hump)
# spine linking the housing down to the core frame
parts.append(box(u(-10), u(10), u(-26), u(-13), u(-20), u(32)))

# vacuum gauge housing
gauge = box(u(-11), u(10), u(-73), u(-53), u(34), u(46.5))
gauge = gauge.edges("|Z").fillet(u(1.5))
gauge = gauge.cut(box(u(-5.5), u(4.5), u(-68), u(-58), u(45), u(48)))
gauge = gauge.cut(box(u(8), u(11), u(-70), u(-56), u(36.5), u(43.5)))
parts.append(gauge)
parts.append(cyl_z(u(-0.5), u(-63), u(0.8), u(44), u(46.5)))
parts.append(box(u(-12.5), u(11.5), u(-74.5), u(-51.5), u(33), u(34)))

# diagonal struts from the crossbar to the pump
for sx in (1, -1):
    parts.append(rod((sx * u(43), u(-46), u(38)), (sx * u(25), u(-46), u(18)), u(1.2)))
    parts.append(cyl_z(sx * u(9), u(-50), u(1.5), u(17), u(31)))

# ---------------- twin pump cylinders -------------------------
for zc in (PUMP_Z, -PUMP_Z):
    c = cyl_x(PUMP_Y, zc, PUMP_R, u(-61), u(54.5))
    c = c.faces("<X").edges().fillet(u(6))
    parts.append(c)
    parts.append(cyl_x(PUMP_Y, zc, u(8.2), u(54.5), u(61.5)))
    parts.append(cyl_x(PUMP_Y, zc, u(10.4), u(-11), u(11)))
    parts.append(cyl_x(PUMP_Y, zc, u(9.8), u(48), u(51)))

# end blocks behind the barrels
parts.append(box(u(14), u(61), u(-45), u(-22), u(-19), u(19)))
parts.append(box(u(-61), u(-40), u(-45), u(-22), u(-19), u(19)))

# ---------------- battery / pump box below ---------------------
parts.append(box(u(-31.7), u(31.7), u(-64), u(-20), u(-38.4), u(-23)))
flange = box(u(-38), u(38), u(-66), u(-20), u(-40.6), u(-38.4))
for hx in (u(-35), u(35)):
    for hy in (u(-63), u(-23)):
        flange = flange.cut(cyl_z(hx, hy, u(1.3), u(-42), u(-38)))
parts.append(flange)
parts.append(box(u(-25.7), u(25.7), u(-58.7), u(-25.2), u(-64.4), u(-40.6)))

# V strap from the block corners up to the pump collar
apex = (u(5), u(-54), u(-19.5))
for ex, ey in ((-33, -64), (33, -64)):
    e = (u(ex), u(ey), u(-22))
    parts.append(rod(e, apex, u(1.0)))
    parts.append(cyl_z(u(ex), u(ey), u(3.0), u(-23), u(-21)))

# fuse everything in one boolean operation
_solids = [p.val() for p in parts]
_fused = _solids[0].fuse(*_solids[1:]).clean()
result = cq.Workplane("XY").add(_fused)
